import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
S = 30.0          # cube edge length
C = 10.9          # corner block size
D = 3.25          # depth of the cross-shaped recesses
CH1 = 2.0         # chamfer on the outer cube edges
CH2 = 1.35        # chamfer on the corner-block edges around the recesses
CI = 0.75         # small chamfer on the inner corners of the cross recesses
FRAME = 19.2      # side of the shallow square panel on the plain faces
FRAME_D = 0.05    # depth of that panel
BOSS_D = 8.25     # peg diameter
BOSS_H = 2.8      # peg height
BOSS_CH = 1.3     # chamfer on the peg end
SEAM_T1 = 3.7     # parting line below the top face (blocks and plain faces)
SEAM_T2 = 2.4     # parting line on the recess floors of the top notches

VIEW = {"azimuth": 45, "elevation": 26}

H = S / 2.0
W = H - C          # half width of the cross arms
M = 0.5            # overshoot of the cutting tools

AX = {0: cq.Vector(1, 0, 0), 1: cq.Vector(0, 1, 0), 2: cq.Vector(0, 0, 1)}

# faces carrying the cross recess: (axis, sign)
RECESSED = {(0, 1), (1, -1), (2, -1)}
# plain faces with panel + peg: (axis, sign)
PEGGED = [(2, 1), (0, -1), (1, 1)]


def prism(a, b, t, pts_ab, t0, t1):
    """Prism whose cross-section is given by global (a, b) coordinates,
    extruded along axis t from t0 to t1."""
    ea, eb, et = AX[a], AX[b], AX[t]
    yd = et.cross(ea)
    sg = yd.dot(eb)
    loc = [(pa, pb * sg) for pa, pb in pts_ab]
    pl = cq.Plane(origin=(0, 0, 0), xDir=ea, normal=et)
    return (cq.Workplane(pl).workplane(offset=t0).polyline(loc).close()
            .extrude(t1 - t0).val())


def slab(ax, sg, lo, hi):
    """Big box limited to lo <= sg*coord[ax] <= hi."""
    big = 2 * S
    dims = [big, big, big]
    dims[ax] = hi - lo
    ctr = [0.0, 0.0, 0.0]
    ctr[ax] = sg * (lo + hi) / 2.0
    return cq.Solid.makeBox(*dims, pnt=cq.Vector(*ctr) - cq.Vector(*dims) * 0.5)


def other(a, b):
    return 3 - a - b


def edge_wedge(a, sa, ua, b, sb, ub, ch, t, t0, t1):
    """Triangular prism cutting a 45 deg chamfer of size ch off the convex edge
    sa*a = ua, sb*b = ub (material on sa*a <= ua and sb*b <= ub), running along t."""
    pts = [(ua - ch - M, ub + M), (ua + M, ub + M), (ua + M, ub - ch - M)]
    pts = [(sa * u, sb * v) for u, v in pts]
    return prism(a, b, t, pts, t0, t1)


# ---------------- base cube with chamfered outer edges ----------------
body = cq.Workplane("XY").box(S, S, S).val()
tools = []
for a in range(3):
    for b in range(a + 1, 3):
        t = other(a, b)
        for sa in (1, -1):
            for sb in (1, -1):
                tools.append(edge_wedge(a, sa, H, b, sb, H, CH1, t, -H - M, H + M))
body = body.cut(*tools).clean()


# ---------------- cross recesses on +X, -Y, -Z ----------------
def cross_pts(w, e, ci):
    """Cross outline (arms of half width w reaching +-e), chamfered inner corners."""
    return [
        (-w, -e), (w, -e), (w, -w - ci), (w + ci, -w), (e, -w), (e, w),
        (w + ci, w), (w, w + ci), (w, e), (-w, e), (-w, w + ci), (-w - ci, w),
        (-e, w), (-e, -w), (-w - ci, -w), (-w, -w - ci),
    ]


tools = []
for (ax, sg) in RECESSED:
    n = AX[ax] * sg
    xd = AX[(ax + 1) % 3]
    pl = cq.Plane(origin=n * (H - D), xDir=xd, normal=n)
    tools.append(cq.Workplane(pl).polyline(cross_pts(W, H + 2, CI)).close()
                 .extrude(D + 2).val())
body = body.cut(*tools).clean()

# ---------------- chamfers on the corner-block edges around the recesses ----------------
tools = []
for sx in (1, -1):
    for sy in (1, -1):
        for sz in (1, -1):
            sgn = {0: sx, 1: sy, 2: sz}
            for a in range(3):              # axis of the inner wall (sgn[a]*a = W)
                for b in range(3):          # recessed face exposing that wall
                    if b == a or (b, sgn[b]) not in RECESSED:
                        continue
                    t = other(a, b)
                    # edge wall / recessed face b, running along t over the block
                    lo, hi = W - M, H + M
                    t0, t1 = (lo, hi) if sgn[t] > 0 else (-hi, -lo)
                    # block material lies on sgn[a]*a >= W and sgn[b]*b <= H
                    pts = [(W + CH2 + M, H + M), (W - M, H + M), (W - M, H - CH2 - M)]
                    tools.append(prism(a, b, t,
                                       [(sgn[a] * u, sgn[b] * v) for u, v in pts], t0, t1))
                    # edge wall / plain face t, only inside the strip of face b
                    if (t, sgn[t]) not in RECESSED:
                        lo, hi = H - D, H + M
                        b0, b1 = (lo, hi) if sgn[b] > 0 else (-hi, -lo)
                        tools.append(prism(a, t, b,
                                           [(sgn[a] * u, sgn[t] * v) for u, v in pts], b0, b1))
            # edges where the exposed walls meet the outer-edge chamfers (CH1 faces)
            for a in range(3):
                b, t = [k for k in range(3) if k != a]
                if (b, sgn[b]) not in RECESSED and (t, sgn[t]) not in RECESSED:
                    continue
                xd = AX[a] * sgn[a]
                yd = (AX[b] * sgn[b] + AX[t] * sgn[t]) * (0.5 ** 0.5)
                w1 = (2 * H - CH1) * (0.5 ** 0.5)
                pl = cq.Plane(origin=(0, 0, 0), xDir=xd, normal=xd.cross(yd))
                pts = [(W - M, w1 + M), (W + CH2 + M, w1 + M), (W - M, w1 - CH2 - M)]
                wedge = (cq.Workplane(pl).polyline(pts).close()
                         .extrude(CH1 * 0.5 ** 0.5 + M, both=True).val())
                rec = [k for k in (b, t) if (k, sgn[k]) in RECESSED]
                if len(rec) == 1:   # keep the wedge inside the strip of that recess
                    wedge = wedge.intersect(slab(rec[0], sgn[rec[0]], H - D, H + 2 * M))
                tools.append(wedge)
body = body.cut(*tools).clean()

# ---------------- plain faces: shallow square panel + chamfered peg ----------------
peg0 = (cq.Workplane("XY").circle(BOSS_D / 2.0).extrude(BOSS_H + FRAME_D)
        .faces(">Z").edges().chamfer(BOSS_CH).val()
        .translate(cq.Vector(0, 0, H - FRAME_D)))
pocket0 = cq.Solid.makeBox(FRAME, FRAME, 1.0, pnt=cq.Vector(-FRAME / 2, -FRAME / 2, H - FRAME_D))
# (axis, angle) taking +Z onto the face normal, and a spin of the peg about its own
# axis that only moves the seam line of its cylindrical faces out of the main views
ROT = {(2, 1): (None, 45), (0, -1): (((0, 1, 0), -90), 180), (1, 1): (((1, 0, 0), -90), 90)}
for key in PEGGED:
    r, spin = ROT[key]
    pk = pocket0
    pg = peg0.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), spin)
    if r is not None:
        pk = pk.rotate(cq.Vector(0, 0, 0), cq.Vector(*r[0]), r[1])
        pg = pg.rotate(cq.Vector(0, 0, 0), cq.Vector(*r[0]), r[1])
    body = body.cut(pk).fuse(pg).clean()

# ---------------- parting lines (face splits only, no change of shape) ----------------
def on_side_floor(e):
    """Edge lying on the floor of the +X or -Y recess."""
    p0, p1 = e.startPoint(), e.endPoint()
    return ((abs(p0.x - (H - D)) < 1e-5 and abs(p1.x - (H - D)) < 1e-5) or
            (abs(p0.y + (H - D)) < 1e-5 and abs(p1.y + (H - D)) < 1e-5))


def add_parting_lines(shape):
    edges = []
    for z0, on_floor in ((H - SEAM_T1, False), (H - SEAM_T2, True)):
        for f in cq.Workplane("XY").add(shape).section(z0).faces().vals():
            edges += [e for e in f.Edges() if on_side_floor(e) == on_floor]
    out = shape.split(*edges).Solids()
    if len(out) == 1 and out[0].isValid() and abs(out[0].Volume() - shape.Volume()) < 1e-6 * shape.Volume():
        return out[0]
    return shape


try:
    body = add_parting_lines(body)
except Exception:
    pass

result = cq.Workplane("XY").newObject([body])
